import cadquery as cq

# ---------------------------------------------------------------
# TV stand with three glass shelves, twin mounting poles and a TV
# X = width (centred), Y = depth (front edge of shelves at Y=0,
# +Y towards the back), Z = up (floor at Z=0).  Units: mm
# ---------------------------------------------------------------

# ---- shelf plan -------------------------------------------------
W = 1500.0          # overall shelf width
D = 570.0           # depth of the centre section
WING_W = 190.0      # width of the cantilevered end wings
WING_D = 380.0      # depth of the end wings
CH = 190.0          # 45 deg chamfer from wing back to centre back
T_SH = 12.0         # shelf (glass) thickness
SH_Z = [64.0, 205.0, 346.0]   # underside height of each shelf
R_SH = 18.0         # plan corner radius of the shelves
TOP = SH_Z[-1] + T_SH          # top surface of the top shelf

# ---- posts --------------------------------------------------------
POST_D = 38.0
COLLAR_D = 46.0
FOOT_D = 56.0
FOOT_H = 14.0
FRONT_POST_X = 527.0
FRONT_POST_Y = 29.0
WING_POST_X = 719.0
WING_POST_Y = 351.0

CAP_D, CAP_H = 30.0, 3.0   # caps on the wing posts
GROM_X = 352.0      # cable grommets at the back corners
GROM_Y = 535.0
GROM_D = 34.0

# ---- twin mounting poles ----------------------------------------
POLE_D = 35.0
POLE_X = 37.5
POLE_Y = 543.0
POLE_TOP = 1488.0

# ---- dividers -----------------------------------------------------
DIV_X = 189.0
DIV_T = 10.0
DIV_Y0, DIV_Y1 = 10.0, 560.0

# ---- top-shelf furniture ------------------------------------------
RAIL_X = 529.0
RAIL_Y0, RAIL_Y1 = 16.0, 78.0
RAIL_H = 38.0
STRIP_X = 371.0
STRIP_Y0, STRIP_Y1 = 335.0, 481.0
STRIP_H = 12.0
HUMP_X = 125.0
HUMP_H = 46.0
HUMP_R = 14.0

# ---- bracket / small platform ------------------------------------
BP_X = 236.0        # half width of back plate
BP_Y0, BP_Y1 = 561.0, 569.0
BP_TOP = 527.0
COL_X = 68.0        # half width of the slot between the side walls
WALL_T = 9.0
COL_Y0 = 481.0
PLAT_X = 128.0
PLAT_Y0, PLAT_Y1 = 387.0, 575.0
PLAT_Z0, PLAT_T = 527.0, 16.0

# ---- television -------------------------------------------------
TV_W = 1334.0
TV_Z0, TV_Z1 = 739.0, 1492.0
TV_Y0, TV_Y1 = 424.0, 460.0
BOX_W = 1132.0
BOX_Z0, BOX_Z1 = 817.0, 1420.0
BOX_Y1 = 528.0
BEZEL = 10.0
BEZEL_TOP = 30.0
BEZEL_BOT = 32.0
CLAMP_X = 200.0
CLAMP_Y1 = 486.0


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl(x, y, z0, z1, d):
    return (cq.Workplane("XY").workplane(offset=z0).center(x, y)
            .circle(d / 2.0).extrude(z1 - z0))


# ---------------------------------------------------------------- shelves
half = W / 2.0
xw = half - WING_W
xc = xw - CH
plan = [(-half, 0), (half, 0), (half, WING_D), (xw, WING_D), (xc, D),
        (-xc, D), (-xw, WING_D), (-half, WING_D)]


def shelf(z0):
    s = (cq.Workplane("XY").workplane(offset=z0).polyline(plan).close()
         .extrude(T_SH))
    s = s.edges("|Z").fillet(R_SH)
    # seam grooves where the glass wings meet the centre panel
    for sx in (-xw, xw):
        s = s.cut(box(sx - 0.6, sx + 0.6, -1, WING_D + 1,
                      z0 + T_SH - 0.8, z0 + T_SH + 1))
        s = s.cut(box(sx - 0.6, sx + 0.6, -1, WING_D + 1,
                      z0 - 1, z0 + 0.8))
    return s


stand = shelf(SH_Z[0])
for z in SH_Z[1:]:
    stand = stand.union(shelf(z))

# ---------------------------------------------------------------- posts


def foot(x, y, d):
    f = cyl(x, y, 0, FOOT_H, d)
    return f.faces(">Z").edges().chamfer(3.0).faces("<Z").edges().chamfer(1.5)


def post(x, y, top):
    p = cyl(x, y, FOOT_H, top, POST_D)
    p = p.union(foot(x, y, FOOT_D))
    # collar sitting on the middle shelf and a flare under the top shelf
    p = p.union(cyl(x, y, SH_Z[1] + T_SH, SH_Z[1] + T_SH + 8, COLLAR_D))
    p = p.union(cyl(x, y, SH_Z[2] - 6, SH_Z[2], COLLAR_D - 4))
    return p


posts = None
for sx in (-1, 1):
    for (px, py) in ((FRONT_POST_X, FRONT_POST_Y),
                     (WING_POST_X, WING_POST_Y)):
        p = post(sx * px, py, TOP)
        posts = p if posts is None else posts.union(p)
stand = stand.union(posts)

# small caps on the wing posts and grommets at the back corners
for sx in (-1, 1):
    stand = stand.union(cyl(sx * WING_POST_X, WING_POST_Y, TOP, TOP + CAP_H, CAP_D))
    stand = stand.cut(cyl(sx * GROM_X, GROM_Y, TOP - 3, TOP + 1, GROM_D))
    stand = stand.union(cyl(sx * GROM_X, GROM_Y, TOP - 4, TOP - 1, GROM_D - 12))

# ---------------------------------------------------------------- dividers
for sx in (-1, 1):
    stand = stand.union(box(sx * DIV_X - DIV_T / 2, sx * DIV_X + DIV_T / 2,
                            DIV_Y0, DIV_Y1, SH_Z[0] + T_SH, SH_Z[2]))

# ---------------------------------------------------------------- front rail
rail = box(-RAIL_X, RAIL_X, RAIL_Y0, RAIL_Y1, TOP, TOP + RAIL_H)
rail = rail.edges("|Z").fillet(10.0).edges(">Z").fillet(4.0)
stand = stand.union(rail)

# ---------------------------------------------------------------- cable cover
strip = box(-STRIP_X, STRIP_X, STRIP_Y0, STRIP_Y1, TOP, TOP + STRIP_H)
strip = strip.edges("|Z").fillet(12.0).edges(">Z").fillet(6.0)
hump = box(-HUMP_X, HUMP_X, STRIP_Y0, STRIP_Y1, TOP, TOP + HUMP_H)
hump = hump.edges("|Y and >Z").fillet(HUMP_R).faces(">Z").edges("|X").fillet(6.0)
stand = stand.union(strip).union(hump)

# ---------------------------------------------------------------- bracket
back_plate = box(-BP_X, BP_X, BP_Y0, BP_Y1, TOP, BP_TOP)
back_plate = back_plate.edges("|Y and >Z").fillet(28.0)
back_plate = back_plate.cut(box(-COL_X + WALL_T, COL_X - WALL_T, BP_Y0 - 1,
                                BP_Y1 + 1, TOP, BP_TOP + 1))
bracket = back_plate
for sx in (-1, 1):
    x_in, x_out = sx * (COL_X - WALL_T), sx * COL_X
    wall = box(min(x_in, x_out), max(x_in, x_out), COL_Y0, BP_Y1, TOP, PLAT_Z0)
    bracket = bracket.union(wall)
plat = box(-PLAT_X, PLAT_X, PLAT_Y0, PLAT_Y1, PLAT_Z0, PLAT_Z0 + PLAT_T)
plat = plat.edges("|Z").fillet(20.0).edges(">Z").fillet(5.0)
bracket = bracket.union(plat)
stand = stand.union(bracket)

# ---------------------------------------------------------------- poles
for sx in (-1, 1):
    pole = cyl(sx * POLE_X, POLE_Y, FOOT_H, POLE_TOP, POLE_D)
    pole = pole.edges(">Z").chamfer(3.0)
    pole = pole.union(foot(sx * POLE_X, POLE_Y, FOOT_D - 4))
    stand = stand.union(pole)

# ---------------------------------------------------------------- TV
panel = box(-TV_W / 2, TV_W / 2, TV_Y0, TV_Y1, TV_Z0, TV_Z1)
panel = panel.edges("|Y").fillet(4.0)
screen = box(-TV_W / 2 + BEZEL, TV_W / 2 - BEZEL, TV_Y0 - 1, TV_Y0 + 3,
             TV_Z0 + BEZEL_BOT, TV_Z1 - BEZEL_TOP)
panel = panel.cut(screen)
back_box = box(-BOX_W / 2, BOX_W / 2, TV_Y1, BOX_Y1, BOX_Z0, BOX_Z1)
back_box = back_box.faces(">Y").edges().chamfer(12.0)
clamp = box(-CLAMP_X, CLAMP_X, TV_Y0 + 1, CLAMP_Y1, TV_Z1 - 4, TV_Z1 + 4.0)
clamp = clamp.union(box(-CLAMP_X, CLAMP_X, TV_Y1, CLAMP_Y1, TV_Z1 - 20, TV_Z1))
clamp = clamp.faces("<X or >X").edges("|Y").chamfer(3.0)
tv = panel.union(back_box).union(clamp)
stand = stand.union(tv)

result = stand

VIEW = {"azimuth": 45, "elevation": 26}
